"""Tubular truss bracket: a thin-walled quad-lobe tube that lofts into a square frame
(triangular side windows, U-slots top and bottom, small corner notches), a clevis with two
lugged side plates, a top cross strip and a floor plate (both with a V cut-out), and a
rectangular sleeve bracket with X-shaped cut-outs in its top and bottom walls.
Axes: X across, Y along the part (tube at Y=0, bracket at +Y), Z up."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 1.2                # sheet thickness of the lofted truss
S = 60.0               # outer size of the square frame
# clover (quad-lobe) tube section at the front end
SIDE_R, SIDE_C = 14.59, 14.28     # side lobes: radius, centre offset in X
TOP_R, TOP_C = 17.79, 8.01        # top/bottom lobes: radius, centre offset in Z
CUSP_R = 0.6           # rounding of the cusps between lobes
SQ_R = 3.0             # corner radius of the square frame
Y_SQ = 122.0           # end of loft / start of square frame
LOFT_MID = [(45.0, 0.52), (80.0, 0.82)]   # (station, blend) of intermediate loft sections
Y_FR = 131.0           # end of the truss (frame end face)

# cut-outs in the truss
SLOT_W = 34.0          # top/bottom U-slot width
SLOT_Y0 = 12.4         # U-slot rounded end
SLOT_Y1 = 122.0        # U-slot square end
TRI_Y0, TRI_Y1, TRI_H = 22.3, 122.0, 24.0   # side triangle apex / base / half-height
HOLE_D, HOLE_Y = 2.5, 5.5
CT_Y, CT_HW, CT_LB, CT_LA = 98.0, 4.2, 2.3, 7.0   # small corner triangles
CT_SH = 1.2            # shift of their base towards the top/bottom face

# clevis plates
PL_T = 2.0
PL_X = 28.8            # outer face of clevis plate (fits inside the frame)
PL_H = 28.8            # top / bottom of the clevis plates
PIN_Y, PIN_Z, PIN_D, LUG_R = 168.1, -20.4, 9.2, 8.6
PL_FLAT_Y = 141.9      # end of the flat top of the clevis plates
PL_ARC_MID = (150.4, 7.5)     # concave flank of the plates (Y, Z): a point on it
PL_ARC_END = (164.5, -9.2)    # ... and its lower end, at the bracket top
STRIP_Y1 = 141.4       # top cross strip of the clevis
CTRI_Y0, CTRI_Y1, CTRI_HW = 132.8, 161.9, 19.85   # clevis V cut (apex, a station, half-width there)
FLOOR_Y1 = 171.8       # end of the clevis floor plate
FL_T = 1.5             # floor / strip thickness
TONGUE_Z0 = -28.0      # underside of the bracket tongue

# bracket
BR_Y0, BR_Y1 = 180.0, 237.0
BR_W, BR_Z0, BR_Z1 = 66.0, -36.0, -9.5
BR_T = 1.5
BR_R = 2.0
TONGUE_Y0 = 162.4
X_ARM_L, X_ARM_W = 60.0, 11.5
X_ANG_A, X_ANG_B = 44.5, -35.8

H = S / 2.0


def circ_inter(c1, r1, c2, r2):
    (x1, y1), (x2, y2) = c1, c2
    d = math.hypot(x2 - x1, y2 - y1)
    a = (r1 * r1 - r2 * r2 + d * d) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    xm, ym = x1 + a * (x2 - x1) / d, y1 + a * (y2 - y1) / d
    return [(xm + h * (y2 - y1) / d, ym - h * (x2 - x1) / d),
            (xm - h * (y2 - y1) / d, ym + h * (x2 - x1) / d)]


def clover_geom(off):
    """key points of the quad-lobe section offset inward by off (cusps rounded)."""
    rs, rt = SIDE_R - off, TOP_R - off
    cs, ct = (SIDE_C, 0.0), (0.0, TOP_C)
    rfo = CUSP_R + off
    fc = max(circ_inter(cs, rs + rfo, ct, rt + rfo), key=lambda p: p[0] + p[1])

    def tp(c, r):
        dx, dy = fc[0] - c[0], fc[1] - c[1]
        d = math.hypot(dx, dy)
        return (c[0] + dx / d * r, c[1] + dy / d * r)

    ps, pt = tp(cs, rs), tp(ct, rt)
    mx, my = (ps[0] + pt[0]) / 2, (ps[1] + pt[1]) / 2
    dx, dy = mx - fc[0], my - fc[1]
    d = math.hypot(dx, dy)
    pm = (fc[0] + dx / d * rfo, fc[1] + dy / d * rfo)
    return rs, rt, ps, pt, pm


def clover_segs(off):
    """8 (start, mid, end) point triples of the quad-lobe section, CCW from the upper-right cusp."""
    rs, rt, ps, pt, pm = clover_geom(off)
    q = lambda p, sx, sz: (p[0] * sx, p[1] * sz)
    return [
        (ps, pm, pt),
        (pt, (0.0, TOP_C + rt), q(pt, -1, 1)),
        (q(pt, -1, 1), q(pm, -1, 1), q(ps, -1, 1)),
        (q(ps, -1, 1), (-SIDE_C - rs, 0.0), q(ps, -1, -1)),
        (q(ps, -1, -1), q(pm, -1, -1), q(pt, -1, -1)),
        (q(pt, -1, -1), (0.0, -TOP_C - rt), q(pt, 1, -1)),
        (q(pt, 1, -1), q(pm, 1, -1), q(ps, 1, -1)),
        (q(ps, 1, -1), (SIDE_C + rs, 0.0), ps),
    ]


def square_segs(off):
    """8 (start, mid, end) triples of the rounded square, same order as clover_segs."""
    h, rc = H - off, SQ_R - off
    a = h - rc
    k = rc * (1 - 1 / math.sqrt(2))
    return [
        ((h, a), (h - k, h - k), (a, h)),
        ((a, h), (0.0, h), (-a, h)),
        ((-a, h), (-h + k, h - k), (-h, a)),
        ((-h, a), (-h, 0.0), (-h, -a)),
        ((-h, -a), (-h + k, -h + k), (-a, -h)),
        ((-a, -h), (0.0, -h), (a, -h)),
        ((a, -h), (h - k, -h + k), (h, -a)),
        ((h, -a), (h, 0.0), (h, a)),
    ]


def section_wire(off, t, y):
    """section blended between the quad-lobe tube (t=0) and the rounded square (t=1) at Y = y."""
    P = lambda p: cq.Vector(p[0], y, p[1])
    lerp = lambda p, r: ((1 - t) * p[0] + t * r[0], (1 - t) * p[1] + t * r[1])
    edges = []
    for sc, ss in zip(clover_segs(off), square_segs(off)):
        a, m, b = (lerp(sc[i], ss[i]) for i in range(3))
        # straight segment when the three points are collinear
        cr = (m[0] - a[0]) * (b[1] - a[1]) - (m[1] - a[1]) * (b[0] - a[0])
        if abs(cr) < 1e-9:
            edges.append(cq.Edge.makeLine(P(a), P(b)))
        else:
            edges.append(cq.Edge.makeThreePointArc(P(a), P(m), P(b)))
    return cq.Wire.assembleEdges(edges)


def truss_solid(off):
    """smooth loft: quad-lobe tube at the front -> rounded square frame at the back."""
    secs = [section_wire(off, 0.0, 0.0)]
    for yy, tt in LOFT_MID:
        secs.append(section_wire(off, tt, yy))
    secs += [section_wire(off, 1.0, Y_SQ), section_wire(off, 1.0, Y_FR)]
    body = cq.Solid.makeLoft(secs, False)
    if off > 0:
        # extend the cavity through both end faces
        front = cq.Solid.makeLoft([section_wire(off, 0.0, -1.0), section_wire(off, 0.0, 0.0)], True)
        back = cq.Solid.makeLoft([section_wire(off, 1.0, Y_FR), section_wire(off, 1.0, Y_FR + 1.0)], True)
        body = body.fuse(front).fuse(back).clean()
    return body


outer = truss_solid(0.0)
inner = truss_solid(T)
truss = cq.Workplane("XY").add(outer.cut(inner))

# side triangles (through X)
tri = (
    cq.Workplane("YZ")
    .polyline([(TRI_Y0, 0), (TRI_Y1, TRI_H), (TRI_Y1, -TRI_H)]).close()
    .extrude(S, both=True)
)
truss = truss.cut(tri)

# top / bottom U-slots (through Z)
slot_tip = (
    cq.Workplane("XY")
    .center(0, SLOT_Y0 + SLOT_W / 2.0)
    .circle(SLOT_W / 2.0)
    .extrude(S, both=True)
)
slot_main = (
    cq.Workplane("XY")
    .center(0, (SLOT_Y0 + SLOT_W / 2.0 + SLOT_Y1) / 2.0)
    .rect(SLOT_W, SLOT_Y1 - SLOT_Y0 - SLOT_W / 2.0)
    .extrude(S, both=True)
    .edges("|Z").fillet(3.0)
)
truss = truss.cut(slot_tip).cut(slot_main)

# small holes near the front, top and bottom
hole = cq.Workplane("XY").center(0, HOLE_Y).circle(HOLE_D / 2.0).extrude(S, both=True)
truss = truss.cut(hole)

# small concave triangles on the four corner rails
_, _, _, _, pm0 = clover_geom(0.0)
tcr = CT_Y / Y_SQ
kq = H - SQ_R * (1 - 1 / math.sqrt(2))
cx = pm0[0] + (kq - pm0[0]) * tcr
cz = pm0[1] + (kq - pm0[1]) * tcr
for sx in (1, -1):
    for sz in (1, -1):
        n = cq.Vector(sx, 0, sz).normalized()
        u = cq.Vector(sx, 0, -sz).normalized()
        pl = cq.Plane(origin=(sx * cx, CT_Y, sz * cz), xDir=u, normal=n)
        k = 0.35
        a, b, c = (-CT_HW - CT_SH, -CT_LB), (CT_HW - CT_SH, -CT_LB), (0.0, CT_LA)
        mid = lambda p, q: ((p[0] + q[0]) / 2 * (1 - k), (p[1] + q[1]) / 2 * (1 - k))
        ctri = (
            cq.Workplane(pl)
            .moveTo(*a)
            .threePointArc(mid(a, b), b)
            .threePointArc(mid(b, c), c)
            .threePointArc(mid(c, a), a)
            .close()
            .extrude(6, both=True)
        )
        truss = truss.cut(ctri)

# ---------------- clevis ----------------
def plate(xo):
    return (
        cq.Workplane("YZ", origin=(xo, 0, 0))
        .moveTo(Y_FR - 0.5, -PL_H)
        .lineTo(Y_FR - 0.5, PL_H)
        .lineTo(PL_FLAT_Y, PL_H)
        .threePointArc(PL_ARC_MID, PL_ARC_END)
        .lineTo(PIN_Y, PIN_Z + LUG_R)
        .threePointArc((PIN_Y + LUG_R, PIN_Z), (PIN_Y, PIN_Z - LUG_R))
        .lineTo(PIN_Y, -PL_H)
        .close()
        .extrude(PL_T)
    )


plates = plate(PL_X - PL_T).union(plate(-PL_X))
IN_W = 2 * (PL_X - PL_T) + 0.2

# tongue between the plates (front part of the bracket)
tongue = (
    cq.Workplane("XY")
    .box(IN_W, BR_Y0 - TONGUE_Y0 + 1.0, BR_Z1 - TONGUE_Z0, centered=(True, False, False))
    .translate((0, TONGUE_Y0, TONGUE_Z0))
)

# floor plate and top cross strip, both with a V cut-out (apex towards the truss)
def clevis_v(z0, z1):
    k = CTRI_HW / (CTRI_Y1 - CTRI_Y0)          # half-width growth per mm
    yb = CTRI_Y0 + (IN_W / 2.0 + 2.0) / k
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .polyline([(0, CTRI_Y0), (IN_W / 2.0 + 2.0, yb), (-IN_W / 2.0 - 2.0, yb)]).close()
        .extrude(z1 - z0)
    )


floor_plate = (
    cq.Workplane("XY", origin=(0, 0, -PL_H))
    .center(0, (Y_FR - 0.5 + FLOOR_Y1) / 2.0)
    .rect(IN_W, FLOOR_Y1 - Y_FR + 0.5)
    .extrude(FL_T)
    .cut(clevis_v(-PL_H - 1, -PL_H + FL_T + 1))
)
top_strip = (
    cq.Workplane("XY", origin=(0, 0, PL_H - FL_T))
    .center(0, (Y_FR - 0.5 + STRIP_Y1) / 2.0)
    .rect(IN_W, STRIP_Y1 - Y_FR + 0.5)
    .extrude(FL_T)
    .cut(clevis_v(PL_H - FL_T - 1, PL_H + 1))
)

# ---------------- bracket ----------------
br_len = BR_Y1 - BR_Y0
br_h = BR_Z1 - BR_Z0
br_outer = (
    cq.Workplane("XY")
    .box(BR_W, br_len, br_h, centered=(True, False, False))
    .translate((0, BR_Y0, BR_Z0))
    .edges("|Y or (|Z and <Y)").fillet(BR_R)
)
br_inner = (
    cq.Workplane("XY")
    .box(BR_W - 2 * BR_T, br_len, br_h - 2 * BR_T, centered=(True, False, False))
    .translate((0, BR_Y0 + BR_T, BR_Z0 + BR_T))
    .edges("|Y").fillet(BR_R - BR_T)
)
bracket = br_outer.cut(br_inner)


def x_cut():
    cy = (BR_Y0 + BR_Y1) / 2.0
    zc = (BR_Z0 + BR_Z1) / 2.0
    arms = None
    for ang in (X_ANG_A, X_ANG_B):
        arm = (
            cq.Workplane("XY", origin=(0, cy, zc))
            .rect(X_ARM_L, X_ARM_W)
            .extrude(br_h, both=True)
            .edges("|Z").fillet(2.5)
            .rotate((0, cy, 0), (0, cy, 1), ang)
        )
        arms = arm if arms is None else arms.union(arm)
    return arms


bracket = bracket.cut(x_cut())

clevis = plates.union(tongue).union(floor_plate).union(top_strip)
pin = cq.Workplane("YZ", origin=(-40, 0, 0)).center(PIN_Y, PIN_Z).circle(PIN_D / 2.0).extrude(80)
clevis = clevis.cut(pin)

result = truss.union(clevis).union(bracket)

VIEW = {"azimuth": 45, "elevation": 26}
